import math
import cadquery as cq

# =============== driving dimensions (mm) ===============
# body outline (front view, XZ), symmetric about X = 0, base at Z = 0
H = 109.0            # body height (base to top flat)
T = 36.0             # body thickness (Y)
HW_BOT = 54.35       # half width at the base
HW_WAIST = 47.15     # half width at the narrowest point of the concave sides
Z_WAIST = 46.0       # height of the narrowest point
Z_BULGE = 86.8       # where the concave side arc runs into the shoulder bulge
R_BULGE = 7.75       # convex radius of the shoulder bulge
ANG_1 = 23.0         # tangent angle (deg) leaving the bulge
ANG_2 = 73.0         # tangent angle (deg) entering the top corner round
TOP_HW = 34.5        # half width of the flat top
R_TOPC = 6.5         # convex radius of the top corner

EDGE_R = 3.0         # fillet on the front/back perimeter (bottom edges stay sharp)

# square pocket in the front (-Y) face
POCKET_W = 65.5
POCKET_H = 65.3
POCKET_Z0 = 14.7     # pocket bottom above the base
POCKET_D = 22.0      # pocket depth

# round boss (cap) on the top
CAP_D = 18.0
CAP_H = 9.3
CAP_TOP_R = 2.25
CAP_BASE_R = 1.5


# =============== outline geometry ===============
def _unit(a_deg):
    a = math.radians(a_deg)
    return (math.cos(a), math.sin(a))


# concave side arc through base corner and waist, centre level with the waist
_dw = HW_BOT - HW_WAIST
R_SIDE = (Z_WAIST ** 2 + _dw ** 2) / (2.0 * _dw)
C_SIDE_X = -(HW_WAIST + R_SIDE)


def side_x(z):
    return C_SIDE_X + math.sqrt(R_SIDE ** 2 - (z - Z_WAIST) ** 2)


def left_profile():
    """Key points of the left half outline (x < 0), walked from the base upward."""
    p0 = (-HW_BOT, 0.0)
    pw = (-HW_WAIST, Z_WAIST)
    q = (side_x(Z_BULGE), Z_BULGE)
    # tangent of side arc at q (walking upward)
    dxdz = -(Z_BULGE - Z_WAIST) / math.sqrt(R_SIDE ** 2 - (Z_BULGE - Z_WAIST) ** 2)
    n = math.hypot(dxdz, 1.0)
    d = (dxdz / n, 1.0 / n)
    # bulge arc (clockwise): centre on the right-hand side of travel
    c = (q[0] + R_BULGE * d[1], q[1] - R_BULGE * d[0])
    a_start = math.atan2(q[1] - c[1], q[0] - c[0])
    e = _unit(ANG_1)
    p2 = (c[0] - R_BULGE * e[1], c[1] + R_BULGE * e[0])
    a_end = math.atan2(p2[1] - c[1], p2[0] - c[0])
    if a_end > a_start:
        a_end -= 2.0 * math.pi
    a_mid = 0.5 * (a_start + a_end)
    m_b = (c[0] + R_BULGE * math.cos(a_mid), c[1] + R_BULGE * math.sin(a_mid))
    # top corner round (clockwise, ends horizontal on the flat top)
    c3 = (-TOP_HW, H - R_TOPC)
    a3s = math.radians(90.0 + ANG_2)
    p3 = (c3[0] + R_TOPC * math.cos(a3s), c3[1] + R_TOPC * math.sin(a3s))
    a3m = math.radians(90.0 + ANG_2 / 2.0)
    m_t = (c3[0] + R_TOPC * math.cos(a3m), c3[1] + R_TOPC * math.sin(a3m))
    p4 = (-TOP_HW, H)
    return p0, pw, q, m_b, p2, p3, m_t, p4


def mx(p):
    return (-p[0], p[1])


p0, pw, q, m_b, p2, p3, m_t, p4 = left_profile()
e1, e2 = _unit(ANG_1), _unit(ANG_2)

# the concave side follows a large circular arc; it is laid down as a smooth
# spline through a few points of that arc (cleaner fillet surfaces)
N_SIDE = 5
SIDE_PTS = [(side_x(Z_BULGE * i / (N_SIDE - 1)), Z_BULGE * i / (N_SIDE - 1)) for i in range(N_SIDE)]


def _side_tangent(z):
    dxdz = -(z - Z_WAIST) / math.sqrt(R_SIDE ** 2 - (z - Z_WAIST) ** 2)
    return (dxdz, 1.0)


T_SIDE0, T_SIDE1 = _side_tangent(0.0), _side_tangent(Z_BULGE)

# closed outline on the XZ plane (plane normal is -Y), centred in thickness
sk = cq.Workplane("XZ", origin=(0, T / 2.0, 0)).moveTo(0, 0).lineTo(*mx(p0))
# right half, going up
sk = sk.spline([mx(p) for p in SIDE_PTS[1:]], tangents=[mx(T_SIDE0), mx(T_SIDE1)], includeCurrent=True)
sk = sk.threePointArc(mx(m_b), mx(p2))
sk = sk.spline([mx(p3)], tangents=[(-e1[0], e1[1]), (-e2[0], e2[1])], includeCurrent=True)
sk = sk.threePointArc(mx(m_t), mx(p4))
# flat top
sk = sk.lineTo(*p4)
# left half, going down
sk = sk.threePointArc(m_t, p3)
sk = sk.spline([p2], tangents=[(-e2[0], -e2[1]), (-e1[0], -e1[1])], includeCurrent=True)
sk = sk.threePointArc(m_b, q)
sk = sk.spline([SIDE_PTS[i] for i in range(len(SIDE_PTS) - 2, -1, -1)],
                tangents=[(-T_SIDE1[0], -T_SIDE1[1]), (-T_SIDE0[0], -T_SIDE0[1])], includeCurrent=True)
sk = sk.close()
body = sk.extrude(T)

# ---- fillet the front and back perimeters, except the straight base edges
y0, y1 = -T / 2.0, T / 2.0


def _perimeter_edge(e):
    ys = [e.positionAt(t).y for t in (0.0, 0.5, 1.0)]
    zs = [e.positionAt(t).z for t in (0.0, 0.5, 1.0)]
    on_front = all(abs(y - y0) < 1e-5 for y in ys)
    on_back = all(abs(y - y1) < 1e-5 for y in ys)
    return (on_front or on_back) and max(zs) > 1e-3


body = body.newObject([e for e in body.edges().vals() if _perimeter_edge(e)]).fillet(EDGE_R)

# ---- cylindrical cap on the top, rounded top edge and blended base
cap = (cq.Workplane("XY", origin=(0, 0, H - 0.5))
       .circle(CAP_D / 2.0).extrude(CAP_H + 0.5)
       .faces(">Z").edges().fillet(CAP_TOP_R))
body = body.union(cap)


def _cap_base(e):
    if e.geomType() != "CIRCLE":
        return False
    c = e.Center()
    return abs(c.z - H) < 1e-5 and abs(c.x) < 1e-5 and abs(c.y) < 1e-5 and abs(e.radius() - CAP_D / 2.0) < 1e-5


body = body.newObject([e for e in body.edges().vals() if _cap_base(e)]).fillet(CAP_BASE_R)

# ---- square pocket sunk into the front (-Y) face
pocket = (cq.Workplane("XZ", origin=(0, -T / 2.0, 0))
          .center(0, POCKET_Z0 + POCKET_H / 2.0)
          .rect(POCKET_W, POCKET_H)
          .extrude(-POCKET_D))
body = body.cut(pocket)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
